import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_NurbsConvert
from OCP.Geom import Geom_BezierCurve
from OCP.GeomConvert import GeomConvert
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.gp import gp_Pnt

# ---------------- driving dimensions (mm) ----------------
skirt_r = 35.1        # outer radius of the shoulder / skirt
skirt_wall = 3.0      # wall thickness of the shoulder
skirt_h = 10.8        # shoulder height (below the rim)
rim_r = 38.3          # outer radius of the base rim / lip
rim_h = 2.4           # rim height
cone_r = 37.9         # base radius of the parabolic nose
cone_h = 105.4        # nose height above the rim
recess_depth = 8.5    # depth of the recess inside the shoulder
pin_d = 4.5           # shear pin hole diameter
pin_z = 5.4           # pin hole centre height above the bottom
pin_count = 2         # pin holes, equally spaced (on the +/-Y axis)
seam_angle = 67.5     # where the revolve seams sit (near the silhouettes of the views)
n_knots = 24          # shape-preserving knots on the nose profile (meshing quality only)

z_rim = skirt_h
z_cone = skirt_h + rim_h
z_tip = z_cone + cone_h


# ---------------- nose: paraboloid (power series n = 1/2) ----------------
def parabola_edge(r0, z0, z1):
    """Exact parabola z = z1 - (z1 - z0) * (r / r0)^2 from (r0, z0) to the tip
    (0, z1): a quadratic Bezier with its middle pole at (r0/2, z1), i.e.
    tangent horizontal at the tip.  Converted to a B-spline with extra knots
    (denser toward the tip); knot insertion does not change the curve."""
    poles = TColgp_Array1OfPnt(1, 3)
    poles.SetValue(1, gp_Pnt(r0, 0, z0))
    poles.SetValue(2, gp_Pnt(r0 / 2.0, 0, z1))
    poles.SetValue(3, gp_Pnt(0, 0, z1))
    curve = GeomConvert.CurveToBSplineCurve_s(Geom_BezierCurve(poles))
    for i in range(1, n_knots - 1):
        s = 1.0 - i / (n_knots - 1.0)
        curve.InsertKnot(1.0 - s * s, 1, 1e-9)
    return cq.Edge(BRepBuilderAPI_MakeEdge(curve).Edge())


nose_wire = cq.Wire.assembleEdges(
    [
        cq.Edge.makeLine(cq.Vector(0, 0, z_tip), cq.Vector(0, 0, z_cone)),
        cq.Edge.makeLine(cq.Vector(0, 0, z_cone), cq.Vector(cone_r, 0, z_cone)),
        parabola_edge(cone_r, z_cone, z_tip),
    ]
)
nose = cq.Solid.revolve(
    cq.Face.makeFromWires(nose_wire), 360, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1)
)
# exact NURBS form of the same solid (meshes more evenly than a revolution surface)
nose = cq.Solid(BRepBuilderAPI_NurbsConvert(nose.wrapped, True).Shape())
nose = cq.Workplane("XY").add(nose)

# ---------------- rim (lip) and shoulder ----------------
rim = cq.Workplane("XY").workplane(offset=z_rim).circle(rim_r).extrude(rim_h)
skirt = cq.Workplane("XY").circle(skirt_r).extrude(skirt_h)

body = nose.union(rim).union(skirt)
body = body.rotate((0, 0, 0), (0, 0, 1), seam_angle)

# ---------------- recess inside the shoulder ----------------
recess = cq.Workplane("XY").circle(skirt_r - skirt_wall).extrude(recess_depth)
body = body.cut(recess)

# ---------------- shear pin holes (radial, through the shoulder wall) ----------------
for k in range(pin_count):
    ang = 90.0 + k * 360.0 / pin_count
    pin = (
        cq.Workplane("XZ", origin=(0, 0, pin_z))
        .circle(pin_d / 2.0)
        .extrude(-(skirt_r + 2.0))          # from the axis out along +Y
        .rotate((0, 0, 0), (0, 0, 1), ang - 90.0)
    )
    body = body.cut(pin)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
